import math
import cadquery as cq

# Display bezel: a rounded-rectangle frame with a crowned top, a window lip,
# a display pocket from below, a cable slot in the front wall and screw holes.

# ---------------- driving dimensions (mm) ----------------
L = 200.0          # overall length (X)
W = 163.0          # overall width  (Y)
H = 23.2           # overall height (Z) at the crest of the top
R_OUT = 7.0        # outer vertical corner radius
R_BOT = 0.8        # round on the outer bottom edge
BOT_RISE = 1.2     # underside rises this much from the pocket edge to the outer edge

WALL = 13.5        # side / back bezel width (top view)
WALL_FRONT = 21.0  # front (-Y) bezel width (top view)
R_IN = 3.0         # window corner radius

EDGE_DROP = 0.6    # outer top edge sits this much below the crest
INNER_DROP = 3.6   # window edge sits this much below the crest
CREST_T = 0.08     # crest position as fraction of bezel width (from outside)

LIP_BOT = 18.0     # underside of the window lip (top of the display pocket)
POCKET_OFF = 4.3   # pocket undercut below the lip (back / sides)
POCKET_OFF_FRONT = 11.8
R_POCKET = 3.0

NOTCH_X0 = -20.5   # cable slot in the front wall, open to the pocket and below
NOTCH_X1 = 17.5
NOTCH_SKIN = 2.5   # wall left standing on the outside of the slot

BACK_HOLE_X = 14.75  # blind holes in the back pocket wall (+/-)
BACK_HOLE_Z = 10.2
BACK_HOLE_D = 4.2
BACK_HOLE_DEPTH = 3.0

FRONT_HOLE_X = (-43.5, 43.5)  # blind holes in the front pocket wall
FRONT_HOLE_Z = 8.5
FRONT_HOLE_D = 3.0
FRONT_HOLE_DEPTH = 3.0

SCREW_D = 3.0      # screw holes in the bottom face
SCREW_DEPTH = 6.0
SCREW_INSET = 4.0
SCREW_FB_X = (-59.0, -30.0, 30.0, 59.0)
SCREW_LR_Y = (-29.5, 29.5)
SCREW_CORNER = (93.0, 74.0)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- helpers ----------------
OUT = (-L / 2, L / 2, -W / 2, W / 2, R_OUT)
WIN = (-L / 2 + WALL, L / 2 - WALL, -W / 2 + WALL_FRONT, W / 2 - WALL, R_IN)


def lerp_rect(a, b, t):
    return tuple(a[i] + (b[i] - a[i]) * t for i in range(5))


def rrect_wire(rc, z):
    x0, x1, y0, y1, r = rc
    V = cq.Vector
    s = math.sqrt(0.5)
    e = [
        cq.Edge.makeLine(V(x0 + r, y0, z), V(x1 - r, y0, z)),
        cq.Edge.makeThreePointArc(V(x1 - r, y0, z), V(x1 - r + r * s, y0 + r - r * s, z), V(x1, y0 + r, z)),
        cq.Edge.makeLine(V(x1, y0 + r, z), V(x1, y1 - r, z)),
        cq.Edge.makeThreePointArc(V(x1, y1 - r, z), V(x1 - r + r * s, y1 - r + r * s, z), V(x1 - r, y1, z)),
        cq.Edge.makeLine(V(x1 - r, y1, z), V(x0 + r, y1, z)),
        cq.Edge.makeThreePointArc(V(x0 + r, y1, z), V(x0 + r - r * s, y1 - r + r * s, z), V(x0, y1 - r, z)),
        cq.Edge.makeLine(V(x0, y1 - r, z), V(x0, y0 + r, z)),
        cq.Edge.makeThreePointArc(V(x0, y0 + r, z), V(x0 + r - r * s, y0 + r - r * s, z), V(x0 + r, y0, z)),
    ]
    return cq.Wire.assembleEdges(e)


def rrect_prism(rc, z0, z1):
    x0, x1, y0, y1, r = rc
    return (cq.Workplane("XY").workplane(offset=z0)
            .center((x0 + x1) / 2, (y0 + y1) / 2)
            .sketch().rect(x1 - x0, y1 - y0).vertices().fillet(r).finalize()
            .extrude(z1 - z0))


def side_faces(solid):
    # the non-horizontal faces of a loft / prism (drops the flat end caps)
    return [f for f in solid.Faces() if f.BoundingBox().zlen > 1e-6]


def loft_faces(wires, ruled=False):
    return side_faces(cq.Solid.makeLoft(wires, ruled))


def prism_faces(wire, h):
    return side_faces(cq.Solid.extrudeLinear(cq.Face.makeFromWires(wire), cq.Vector(0, 0, h)))


def section(t, z):
    # outline offset a fraction t of the way from the outer edge to the window edge
    return rrect_wire(lerp_rect(OUT, WIN, t), z)


# ---------------- bezel body ----------------
# One closed shell: outer wall, crowned top (lofted through a few offsets of the
# outline: a short rise from the outer edge to the crest, then a long convex fall to
# the window edge), window lip, display pocket and a slightly sloped underside.
POCKET = (WIN[0] - POCKET_OFF, WIN[1] + POCKET_OFF, WIN[2] - POCKET_OFF_FRONT, WIN[3] + POCKET_OFF, R_POCKET)


tc = CREST_T
faces = []
faces += loft_faces([section(0.0, H - EDGE_DROP), section(0.4 * tc, H - 0.36 * EDGE_DROP), section(tc, H)])
faces += loft_faces([section(tc, H), section((1 + tc) / 2, H - 0.25 * INNER_DROP), section(1.0, H - INNER_DROP)])
faces += prism_faces(rrect_wire(OUT, BOT_RISE), H - EDGE_DROP - BOT_RISE)          # outer wall
faces += prism_faces(rrect_wire(WIN, LIP_BOT), H - INNER_DROP - LIP_BOT)          # window edge of the lip
faces.append(cq.Face.makeFromWires(rrect_wire(POCKET, LIP_BOT), [rrect_wire(WIN, LIP_BOT)]))  # lip underside
faces += prism_faces(rrect_wire(POCKET, 0.0), LIP_BOT)                             # pocket wall
faces += loft_faces([rrect_wire(OUT, BOT_RISE), rrect_wire(POCKET, 0.0)], ruled=True)  # underside

body = cq.Workplane("XY").add(cq.Solid.makeSolid(cq.Shell.makeShell(faces)))

# small round on the outer bottom edge
bot_edges = [e for e in body.val().Edges()
             if abs(e.Center().z - BOT_RISE) < 1e-6
             and (abs(e.Center().x) > L / 2 - 3 or abs(e.Center().y) > W / 2 - 3)]
body = cq.Workplane("XY").add(body.val().fillet(R_BOT, bot_edges))

# cable slot through the front wall (open to the pocket and to the underside)
slot = (cq.Workplane("XY")
        .box(NOTCH_X1 - NOTCH_X0, WALL_FRONT, LIP_BOT + 1.0, centered=False)
        .translate((NOTCH_X0, -W / 2 + NOTCH_SKIN, -1.0)))
body = body.cut(slot)

# blind holes in the back pocket wall (XZ workplane normal is -Y)
for hx in (-BACK_HOLE_X, BACK_HOLE_X):
    hole = (cq.Workplane("XZ", origin=(hx, POCKET[3] - 0.5, BACK_HOLE_Z))
            .circle(BACK_HOLE_D / 2).extrude(-(BACK_HOLE_DEPTH + 0.5)))
    body = body.cut(hole)

# blind holes in the front pocket wall
for hx in FRONT_HOLE_X:
    hole = (cq.Workplane("XZ", origin=(hx, POCKET[2] + 0.5, FRONT_HOLE_Z))
            .circle(FRONT_HOLE_D / 2).extrude(FRONT_HOLE_DEPTH + 0.5))
    body = body.cut(hole)

# screw holes in the bottom face
pts = []
for x in SCREW_FB_X:
    pts.append((x, -W / 2 + SCREW_INSET))
    pts.append((x, W / 2 - SCREW_INSET))
for y in SCREW_LR_Y:
    pts.append((-L / 2 + SCREW_INSET, y))
    pts.append((L / 2 - SCREW_INSET, y))
for sx in (-1, 1):
    for sy in (-1, 1):
        pts.append((sx * SCREW_CORNER[0], sy * SCREW_CORNER[1]))
screws = (cq.Workplane("XY").workplane(offset=-1.0).pushPoints(pts)
          .circle(SCREW_D / 2).extrude(SCREW_DEPTH + 1.0))
body = body.cut(screws)

result = body
